import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
ROT_Z = 11.0            # the whole part is turned about Z in the target orientation

# fork (inverted U at the bottom)
FORK_TOP_Z = 72.0
FORK_TOP_HALF = 44.5    # half width at the top of the cross bar
FORK_HALF = 50.0        # half width over the legs (outer)
FORK_SHOULDER_Z = 45.0  # outer slant meets the vertical leg side
LEG_INNER = 34.1        # half width of the opening between the legs
SLOT_TOP_Z = 56.7       # underside of the cross bar
SLOT_TOP_HALF = 23.4    # half width of the flat underside
SLOT_SLANT_Z = 35.0     # inner slant meets the vertical leg side
FORK_DEPTH = 21.0
FORK_CORNER_R = 4.0     # profile corner rounding (opening side)
FORK_SHOULDER_R = 1.5   # rounding of the outer top corners
FORK_FILLET = 2.5       # edge rounding of the fork body

# column (flat bar with a channel down its back)
COL_HALF = 31.7
COL_Y0, COL_Y1 = -6.0, 4.8
COL_TOP_Z = 205.5
COL_FILLET = 2.0
CHAN_X0, CHAN_X1 = -15.5, 13.0
CHAN_DEPTH = 5.5

# ledge between column and header
LEDGE_HALF = 32.5
LEDGE_Y0, LEDGE_Y1 = -10.0, COL_Y1
LEDGE_TOP_Z = 209.9

# header box with two jack openings
HEAD_HALF = 37.25
HEAD_DEPTH = 21.5
HEAD_TOP_Z = 237.8
HEAD_EDGE_R = 0.8
POCKET_X = (-33.3, 2.2)     # left edge of each jack opening
POCKET_W = 29.8
POCKET_Z0, POCKET_Z1 = 211.0, 233.0
# stepped side bulges of the openings: (extra left, extra right, inset from top/bottom)
POCKET_STEPS = ((0.6, 0.6, 2.5), (1.0, 1.0, 6.5))
POCKET_DEPTH = 14.5
END_HOLE_D = 3.6
END_HOLE_Y = -1.5
END_HOLE_Z = (212.9, 230.8)
BACK_SLOT = (-35.5, -27.5, 234.3, 235.9)   # x0, x1, z0, z1 on the back face

# leg end features
LEG_END_R = FORK_DEPTH / 2.0
DISK_R = 9.2
DISK_T = 0.8
DISK_HOLE_PCD_R = 5.8
DISK_HOLE_D = 1.8
CSK_PITCH = 4.7
CSK_D, CSK_HEAD_D = 2.8, 5.0
LATCH_DEPTH = 1.5
LATCH_H = 9.0

# thin slot in the top of the fork in front of the column
TOP_SLOT = (-24.4, -6.4, -8.8, -8.0)    # x0, x1, y0, y1
TOP_SLOT_DEPTH = 2.0

# bracket on the back of the -X leg
BRACKET = (-46.0, -36.0, 39.0, 49.0)      # x0, x1, z0, z1
BRACKET_PROUD = 4.5


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def x_cyl(x0, length, y, z, r):
    """Cylinder along +X starting at x0."""
    return cq.Workplane("YZ").workplane(offset=x0).center(y, z).circle(r).extrude(length)


def csk_tool(x_face, sx, y, z):
    """Countersunk hole entering a face at x = x_face whose outward normal is sx*X."""
    d = cq.Vector(-sx, 0, 0)
    p = cq.Vector(x_face + sx * 0.01, y, z)
    hr = CSK_HEAD_D / 2.0
    cone = cq.Solid.makeCone(hr + 0.01, 0.0, hr + 0.01, p, d)
    shaft = cq.Solid.makeCylinder(CSK_D / 2.0, 5.0, p, d)
    return cq.Workplane("XY").add(cone.fuse(shaft))


class _AboveZ(cq.Selector):
    def __init__(self, z):
        self.z = z

    def filter(self, objs):
        return [o for o in objs if o.Center().z > self.z]


class _NearX(cq.Selector):
    """Keep objects with |x| beyond (outer=True) or within (outer=False) a limit."""
    def __init__(self, lim, outer):
        self.lim, self.outer = lim, outer

    def filter(self, objs):
        return [o for o in objs if (abs(o.Center().x) > self.lim) == self.outer]


# ---------------- fork ----------------
fork_pts = [
    (-FORK_TOP_HALF, FORK_TOP_Z), (FORK_TOP_HALF, FORK_TOP_Z),
    (FORK_HALF, FORK_SHOULDER_Z), (FORK_HALF, 0.0),
    (LEG_INNER, 0.0), (LEG_INNER, SLOT_SLANT_Z),
    (SLOT_TOP_HALF, SLOT_TOP_Z), (-SLOT_TOP_HALF, SLOT_TOP_Z),
    (-LEG_INNER, SLOT_SLANT_Z), (-LEG_INNER, 0.0),
    (-FORK_HALF, 0.0), (-FORK_HALF, FORK_SHOULDER_Z),
]
fork = (cq.Workplane("XZ").polyline(fork_pts).close()
        .extrude(FORK_DEPTH / 2.0, both=True))
fork = fork.edges("|Y").edges(_AboveZ(1.0)).edges(_NearX(40.0, False)).fillet(FORK_CORNER_R)
fork = fork.edges("|Y").edges(_AboveZ(FORK_TOP_Z - 1.0)).edges(_NearX(40.0, True)).fillet(FORK_SHOULDER_R)

# leg ends are full rounds about X
_span = 2 * FORK_HALF + 10
stadium = (box(-_span / 2, _span / 2, -FORK_DEPTH / 2, FORK_DEPTH / 2, LEG_END_R, FORK_TOP_Z + 20)
           .union(x_cyl(-_span / 2, _span, 0, LEG_END_R, LEG_END_R)))
fork = fork.intersect(stadium)
fork = fork.edges().fillet(FORK_FILLET)

# ---------------- column ----------------
column = (box(-COL_HALF, COL_HALF, COL_Y0, COL_Y1, FORK_TOP_Z - 1.0, COL_TOP_Z)
          .edges("|Z and <Y").fillet(COL_FILLET))
ledge = box(-LEDGE_HALF, LEDGE_HALF, LEDGE_Y0, LEDGE_Y1, COL_TOP_Z - 0.5, LEDGE_TOP_Z)
column = column.union(ledge)
# channel runs from the fork up to the underside of the header
column = column.cut(box(CHAN_X0, CHAN_X1, COL_Y1 - CHAN_DEPTH, COL_Y1 + 1,
                        FORK_TOP_Z, LEDGE_TOP_Z))

# ---------------- header ----------------
hy0, hy1 = -HEAD_DEPTH / 2.0, HEAD_DEPTH / 2.0
header = box(-HEAD_HALF, HEAD_HALF, hy0, hy1, LEDGE_TOP_Z, HEAD_TOP_Z)
header = header.faces("<X or >X").edges().fillet(HEAD_EDGE_R)
for xa in POCKET_X:
    # jack opening: rectangle with stepped bulges on both sides at mid height
    xb = xa + POCKET_W
    header = header.cut(box(xa, xb, hy0 - 1, hy0 + POCKET_DEPTH, POCKET_Z0, POCKET_Z1))
    for el, er, dz in POCKET_STEPS:
        header = header.cut(box(xa - el, xb + er, hy0 - 1, hy0 + POCKET_DEPTH,
                                POCKET_Z0 + dz, POCKET_Z1 - dz))
# screw holes in both end faces
for sx in (-1, 1):
    x_start = HEAD_HALF - 5.0 if sx > 0 else -HEAD_HALF - 1.0
    for z in END_HOLE_Z:
        header = header.cut(x_cyl(x_start, 6.0, END_HOLE_Y, z, END_HOLE_D / 2))
# small slot in the back face
bx0, bx1, bz0, bz1 = BACK_SLOT
header = header.cut(box(bx0, bx1, hy1 - 2.0, hy1 + 1.0, bz0, bz1))

part = fork.union(column).union(header)
tx0, tx1, ty0, ty1 = TOP_SLOT
part = part.cut(box(tx0, tx1, ty0, ty1, FORK_TOP_Z - TOP_SLOT_DEPTH, FORK_TOP_Z + 1.0))

# ---------------- leg end details ----------------
for sx in (-1, 1):
    x_in = sx * LEG_INNER
    # raised pivot disk on the inner face of each leg
    disk_x0 = x_in - DISK_T if sx > 0 else x_in
    part = part.union(x_cyl(disk_x0, DISK_T, 0, LEG_END_R, DISK_R))
    # latch recess in front of the disk with a small hook
    if sx > 0:
        rx0, rx1 = x_in - DISK_T - 0.1, x_in + LATCH_DEPTH
    else:
        rx0, rx1 = x_in - LATCH_DEPTH, x_in + DISK_T + 0.1
    part = part.cut(box(rx0, rx1, -LEG_END_R - 1, -2.0,
                        LEG_END_R - LATCH_H / 2, LEG_END_R + LATCH_H / 2))
    hook = (cq.Workplane("XY").box(LATCH_DEPTH, 6.5, 1.8)
            .rotate((0, 0, 0), (1, 0, 0), 35)
            .translate((x_in + sx * LATCH_DEPTH / 2, -3.2, LEG_END_R)))
    part = part.union(hook)
    for k in range(4):
        a = math.radians(45 + 90 * k)
        yy = DISK_HOLE_PCD_R * math.cos(a)
        zz = LEG_END_R + DISK_HOLE_PCD_R * math.sin(a)
        part = part.cut(x_cyl(x_in - 3, 6, yy, zz, DISK_HOLE_D / 2))
    # countersunk hole pattern on the outer face
    x_out = sx * FORK_HALF
    for yy in (-CSK_PITCH, CSK_PITCH):
        for zz in (LEG_END_R - CSK_PITCH, LEG_END_R + CSK_PITCH):
            part = part.cut(csk_tool(x_out, sx, yy, zz))
    part = part.cut(x_cyl(x_out - 3, 6, 0, LEG_END_R, 0.8))

# small slotted bracket on the back of the -X leg
kx0, kx1, kz0, kz1 = BRACKET
bracket = box(kx0, kx1, FORK_DEPTH / 2 - 1.5, FORK_DEPTH / 2 + BRACKET_PROUD, kz0, kz1)
bracket = bracket.cut(box(kx1 - 3.2, kx1 - 2.4, FORK_DEPTH / 2, FORK_DEPTH / 2 + BRACKET_PROUD + 1,
                          kz0 - 1, kz1 + 1))
part = part.union(bracket)

result = part.rotate((0, 0, 0), (0, 0, 1), ROT_Z)
